import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 236.0            # overall width  (X)
D = 188.0            # overall depth  (Y)
T = 5.0              # top plate / rib thickness (top of plate at Z=0)
BAND_SIDE = 10.4     # band width along the two sides
BAND_BACK = 10.0     # band width along the back
BAND_FRONT = 5.5     # band width along the front
R_OUT = 47.0         # outer radius of the two back corners
R_IN = 38.5          # inner radius of the two back corners
R_FRONT = 4.0        # small radius on the front outer corners

WALL_T = 3.5         # thin wall thickness (walls hang under the band)
WALL_BOT = -16.8     # underside of the walls
END_LEN = 4.5        # length of the full-width block at the wall ends
END_R = 1.0          # rounding of the convex pocket-end corner
POCKET_R = 1.2       # rounding of the concave pocket corners
END_FILLET = 4.5     # fillet between a wall end face and the band underside

SIDE_WALL_END = D / 2 - R_OUT       # side walls run from the front edge to here
BACK_WALL_HALF = W / 2 - R_OUT      # back wall half length

BOSS_R = 8.75        # corner boss radius
BOSS_LEN = 15.0      # all bosses are the same length ...
# ... but sit at different heights: top of each corner boss above the plate
BOSS_TOP_FL = 2.6    # front-left
BOSS_TOP_BL = 1.85   # back-left
BOSS_TOP_FR = 0.6    # front-right
BOSS_TOP_BR = 0.4    # back-right
BOSS_X = 100.0
BOSS_Y_BACK = D / 2 - 27.0
BOSS_Y_FRONT = -D / 2 + 13.1

MID_R = 8.8          # back middle boss
MID_Y = D / 2 - 15.0
MID_TOP = 0.4        # middle boss top sits just proud of the band
MID_BOT = MID_TOP - BOSS_LEN
MID_FILLET = 2.0     # blend of the middle boss into the band

HUB_R = 8.5          # central hub under the rib crossing
HUB_BOT = -15.5
HUB_HOLE_D = 6.0
HUB_HOLE_DEPTH = 6.0

RIB_W = 7.7
RIB_CROTCH_R = 4.8   # fillets in the crossing of the ribs (top view)
RIB_BOT_R = 2.0      # rounded underside edges of the ribs
EDGE_R = 1.0         # small edge break on the top edges of band and ribs

HOLE_D = 5.0         # threaded holes in the walls (thread itself omitted)
CSK_D = 9.6          # countersink on the outside
HOLE_Z = (-T + WALL_BOT) / 2.0
SIDE_HOLE_Y = [-D / 2 + 10.8, -D / 2 + 123.3]
BACK_HOLE_X = [-47.5, 47.5]


# ---------------- helpers ----------------
def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


SEAM_DEG = 135.0      # put cylinder seams on the back-left side


def cyl(x, y, r, z0, z1):
    c = (cq.Workplane("XY").workplane(offset=z0)
         .circle(r).extrude(z1 - z0)
         .rotate((0, 0, 0), (0, 0, 1), SEAM_DEG))
    return c.translate((x, y, 0))


def near_edge(pt):
    return cq.selectors.NearestToPointSelector(pt)


def outer_prism(z0, z1):
    p = box(-W / 2, W / 2, -D / 2, D / 2, z0, z1)
    p = p.edges("|Z and >Y").fillet(R_OUT)
    p = p.edges("|Z and <Y").fillet(R_FRONT)
    return p


def inner_prism(z0, z1):
    p = box(-W / 2 + BAND_SIDE, W / 2 - BAND_SIDE,
            -D / 2 + BAND_FRONT, D / 2 - BAND_BACK, z0, z1)
    p = p.edges("|Z and >Y").fillet(R_IN)
    return p


# ---------------- top frame plate (band) ----------------
# The opening inside the band is notched around every boss (the bosses
# merge into the band with small blends), the front inner corners are
# filled up to the front bosses.
XI = W / 2 - BAND_SIDE          # inner side edge
YF = -D / 2 + BAND_FRONT        # inner front edge
YB = D / 2 - BAND_BACK          # inner back edge
ARC_C = (XI - R_IN, YB - R_IN)  # centre of the +X inner back arc
NOTCH_DR = 0.5                  # notch radius is a little under the boss radius


def _circle_hits(c0, r0, c1, r1):
    dx, dy = c1[0] - c0[0], c1[1] - c0[1]
    d = math.hypot(dx, dy)
    a = (r0 ** 2 - r1 ** 2 + d ** 2) / (2 * d)
    h = math.sqrt(max(r0 ** 2 - a ** 2, 0.0))
    mx, my = c0[0] + a * dx / d, c0[1] + a * dy / d
    return [(mx + h * dy / d, my - h * dx / d), (mx - h * dy / d, my + h * dx / d)]


def _blend(solid, pts, r):
    for p in pts:
        try:
            solid = solid.edges("|Z").edges(near_edge((p[0], p[1], -T / 2))).fillet(r)
        except Exception:
            print("blend failed at", p)
    return solid


opening = inner_prism(-T - 1, 1)
blend_pts = []
# middle boss at the back
_rb = MID_R - NOTCH_DR
opening = opening.cut(cyl(0, MID_Y, _rb, -T - 2, 2))
_xj = math.sqrt(max(_rb ** 2 - (MID_Y - YB) ** 2, 0.0))
blend_pts += [(-_xj, YB), (_xj, YB)]
# corner bosses
_rc = BOSS_R - NOTCH_DR
for sx in (-1, 1):
    # front corner: notch + fill the little corner left between boss and band
    cx, cy = sx * BOSS_X, BOSS_Y_FRONT
    opening = opening.cut(cyl(cx, cy, _rc, -T - 2, 2))
    opening = opening.cut(box(min(cx, sx * (XI + 1)), max(cx, sx * (XI + 1)),
                              YF - 1, cy, -T - 2, 2))
    blend_pts.append((sx * XI, cy + math.sqrt(_rc ** 2 - (XI - BOSS_X) ** 2)))
    blend_pts.append((cx - sx * math.sqrt(_rc ** 2 - (cy - YF) ** 2), YF))
    # back corner: notch into the inner arc
    cx, cy = sx * BOSS_X, BOSS_Y_BACK
    opening = opening.cut(cyl(cx, cy, _rc, -T - 2, 2))
    arc_c = (sx * ARC_C[0], ARC_C[1])
    blend_pts += _circle_hits((cx, cy), _rc, arc_c, R_IN)
opening = _blend(opening, blend_pts, MID_FILLET)
plate = outer_prism(-T, 0).cut(opening)
try:
    plate = plate.faces(">Z").edges().fillet(EDGE_R)
except Exception:
    print("plate edge fillet failed")

# ---------------- walls under the band ----------------
ZM = (WALL_BOT - T) / 2.0


def side_wall_pos():
    """+X wall: thin wall flush with the outside, a short full-width block
    at its back end (pocket on the inside with rounded corners)."""
    xo, xi = W / 2, W / 2 - BAND_SIDE
    y0, y1 = -D / 2, SIDE_WALL_END
    w = box(xi, xo, y0, y1, WALL_BOT, -T)
    xt = W / 2 - WALL_T
    yp = y1 - END_LEN
    pk = box(xi - 1.0, xt, y0 - 1.0, yp, WALL_BOT - 1, -T)
    pk = pk.edges("|Z").edges(near_edge((xt, yp, ZM))).fillet(POCKET_R)
    w = w.cut(pk)
    w = w.edges("|Z").edges(near_edge((xi, yp, ZM))).fillet(END_R)
    return w


def back_wall():
    yo, yi = D / 2, D / 2 - BAND_BACK
    x0, x1 = -BACK_WALL_HALF, BACK_WALL_HALF
    w = box(x0, x1, yi, yo, WALL_BOT, -T)
    yt = D / 2 - WALL_T
    pk = box(x0 + END_LEN, x1 - END_LEN, yi - 1.0, yt, WALL_BOT - 1, -T)
    for xe in (x0 + END_LEN, x1 - END_LEN):
        pk = pk.edges("|Z").edges(near_edge((xe, yt, ZM))).fillet(POCKET_R)
    w = w.cut(pk)
    for xe in (x0 + END_LEN, x1 - END_LEN):
        w = w.edges("|Z").edges(near_edge((xe, yi, ZM))).fillet(END_R)
    return w


def straight_fillet_x(x0, x1, y_face, direction):
    """Concave fillet wedge along X under the band at a wall end face
    lying in the plane y=y_face, growing toward +Y (direction=+1) or -Y."""
    R = END_FILLET
    ya, yb = (y_face, y_face + R) if direction > 0 else (y_face - R, y_face)
    blk = box(x0, x1, ya, yb, -T - R, -T)
    cut = (cq.Workplane("YZ").workplane(offset=x0 - 1)
           .center(y_face + direction * R, -T - R).circle(R).extrude(x1 - x0 + 2))
    return blk.cut(cut)


def straight_fillet_y(y0, y1, x_face, direction):
    """Same as straight_fillet_x for a wall end face in the plane x=x_face."""
    R = END_FILLET
    xa, xb = (x_face, x_face + R) if direction > 0 else (x_face - R, x_face)
    blk = box(xa, xb, y0, y1, -T - R, -T)
    cut = (cq.Workplane("XZ").workplane(offset=-(y1 + 1))
           .center(x_face + direction * R, -T - R).circle(R).extrude(y1 - y0 + 2))
    return blk.cut(cut)


# end fillet of the +X side wall (towards +Y) and of the back wall (+X end)
ef_side = straight_fillet_x(W / 2 - BAND_SIDE - 1, W / 2 + 1, SIDE_WALL_END, +1)
ef_back = straight_fillet_y(D / 2 - BAND_BACK - 1, D / 2 + 1, BACK_WALL_HALF, +1)

wall_p = side_wall_pos().union(ef_side)
wall_n = wall_p.mirror("YZ")
wall_b = back_wall().union(ef_back).union(ef_back.mirror("YZ"))

walls = wall_p.union(wall_n).union(wall_b)
# keep all wall material strictly under the band
band_zone = outer_prism(WALL_BOT - 1, -T + 0.5).cut(inner_prism(WALL_BOT - 2, 1))
walls = walls.intersect(band_zone)

body = plate.union(walls)

# ---------------- bosses ----------------
corner_bosses = [
    (-BOSS_X, BOSS_Y_FRONT, BOSS_TOP_FL),
    (-BOSS_X, BOSS_Y_BACK, BOSS_TOP_BL),
    (BOSS_X, BOSS_Y_FRONT, BOSS_TOP_FR),
    (BOSS_X, BOSS_Y_BACK, BOSS_TOP_BR),
]
for bx, by, btop in corner_bosses:
    body = body.union(cyl(bx, by, BOSS_R, btop - BOSS_LEN, btop))

body = body.union(cyl(0, MID_Y, MID_R, MID_BOT, MID_TOP))

# ---------------- diagonal ribs with central hub ----------------
p_fl = (-BOSS_X, BOSS_Y_FRONT)
p_br = (BOSS_X, BOSS_Y_BACK)
hub_y = (BOSS_Y_BACK + BOSS_Y_FRONT) / 2.0
rib_len = math.hypot(p_br[0] - p_fl[0], p_br[1] - p_fl[1])
rib_ang = math.degrees(math.atan2(p_br[1] - p_fl[1], p_br[0] - p_fl[0]))


class _NearOrigin(cq.Selector):
    def __init__(self, r):
        self.r = r

    def filter(self, objs):
        return [o for o in objs if math.hypot(o.Center().x, o.Center().y) < self.r]


cross_sk = (cq.Sketch()
            .rect(rib_len, RIB_W, angle=rib_ang)
            .rect(rib_len, RIB_W, angle=-rib_ang)
            .clean()
            .vertices(_NearOrigin(12.0)).fillet(RIB_CROTCH_R))
cross = cq.Workplane("XY").workplane(offset=-T).placeSketch(cross_sk).extrude(T)
try:
    cross = cross.faces("<Z").edges().fillet(RIB_BOT_R)
except Exception:
    print("rib fillet failed")
try:
    cross = cross.faces(">Z").edges().fillet(EDGE_R)
except Exception:
    print("rib top fillet failed")
cross = cross.translate((0, hub_y, 0))
cross = cross.union(cyl(0, hub_y, HUB_R, HUB_BOT, 0))
body = body.union(cross)

# blind hole in the hub
body = body.cut(cyl(0, hub_y, HUB_HOLE_D / 2, -HUB_HOLE_DEPTH, 1))

# ---------------- countersunk holes through the walls ----------------
for sx in (-1, 1):
    for yh in SIDE_HOLE_Y:
        x_a = sx * (W / 2 + 2)
        x_b = sx * (W / 2 - WALL_T - 1)
        drill = (cq.Workplane("YZ").workplane(offset=min(x_a, x_b))
                 .center(yh, HOLE_Z).circle(HOLE_D / 2).extrude(abs(x_a - x_b)))
        csk = cq.Workplane("XY").add(cq.Solid.makeCone(
            CSK_D / 2, 0, CSK_D / 2,
            pnt=cq.Vector(sx * (W / 2 + 0.01), yh, HOLE_Z),
            dir=cq.Vector(-sx, 0, 0)))
        body = body.cut(drill).cut(csk)

for xh in BACK_HOLE_X:
    drill = (cq.Workplane("XZ").workplane(offset=-D / 2 - 2)
             .center(xh, HOLE_Z).circle(HOLE_D / 2).extrude(WALL_T + 3))
    csk = cq.Workplane("XY").add(cq.Solid.makeCone(
        CSK_D / 2, 0, CSK_D / 2,
        pnt=cq.Vector(xh, D / 2 + 0.01, HOLE_Z),
        dir=cq.Vector(0, -1, 0)))
    body = body.cut(drill).cut(csk)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
